import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 200.0          # outer length (X)
W = 139.4          # outer width (Y)
H = 24.3           # outer height (Z)
T_WALL = 2.0       # side wall thickness
T_FLOOR = 2.0      # floor thickness
R_CORNER = 0.0     # outer vertical edge round (0 = sharp)
RIM_CHAMFER = 1.0  # 45 deg chamfer on the outer top edge
POST_TOP = H - 0.8 # top of the screw posts

# corner screw posts
POST_INSET = 7.6   # post centre from outer faces
POST_D = 6.5
POST_HOLE_D = 2.6
POST_HOLE_DEPTH = 12.0
POST_CSK_D = 3.6   # small 90 deg countersink at the mouth of the post holes
POST_FILLET = 1.7  # concave fillet at the foot of the posts

# PCB stand-offs on the floor (through holes)
BOSS_PTS = [(-84.2, -52.4), (-84.5, 58.5), (53.5, -52.5), (33.1, 58.5)]
BOSS_D = 4.5
BOSS_H = 2.9
BOSS_FLARE_W = 1.3
BOSS_FLARE_H = 1.3
BOSS_HOLE_D = 2.5
BOSS_CSK_D = 4.5   # countersink of the stand-off holes on the underside

# divider wall
DIV_X = 62.2
DIV_T = 1.6        # divider thickness
DIV_FILLET = 1.2   # fillet between divider and floor
DIV_WIN_Y = 30.5   # centre of small window in the divider
DIV_WIN_Z = 12.5
DIV_WIN_S = 6.4

# post in the right compartment
POST2_X, POST2_Y = 81.0, 0.0
POST2_TOP = H - 1.3

# connector cut-outs in the front wall (x-centre, width)
CUT_Z0 = 6.0       # bottom of cut-out
CUT_H = 10.0       # height of main rectangle
NOTCH_W = 3.8
NOTCH_H = 4.8
NOTCH_R = 0.9      # rounded shoulders where the notch meets the rectangle
CUT_RECESS = 1.0   # depth of the outer recess (notch is blind)
CUT_RECESS_IN = 0.6  # depth of the matching recess on the inner face
CUT_LIP = 1.2      # through opening is this much shorter at the top
CUTS = [(-74.9, 10.0),
        (-59.6, 9.9), (-48.6, 9.9),
        (-34.3, 9.9), (-23.6, 9.9),
        (-10.0, 9.9), (0.9, 9.9),
        (18.3, 17.8), (37.0, 17.8)]

# window in back wall
BACK_WIN_X = 55.5
BACK_WIN_W = 9.5
BACK_WIN_Z0 = 6.0
BACK_WIN_H = 10.0

# mounting tabs on both X ends
TAB_T = 2.0
TAB_OUT = 11.8     # protrusion beyond the wall
TAB_BASE = 64.5    # width along the wall
TAB_TIP = 45.5     # width at the outer edge
TAB_HOLE_X = 6.0   # hole centre from the wall
TAB_HOLE_Y = 18.0
TAB_HOLE_D = 3.2
TAB_CSK_D = 6.0
TAB_FILLET = 2.0   # fillet between tab and wall
TAB_CORNER_R = 1.0 # round on the tab tip corners
TAB_EDGE_R = 0.5   # round on the upper outer edges of the tab

# ---------------- body ----------------
outer = (cq.Workplane("XY").rect(L, W).extrude(H)
         .faces(">Z").chamfer(RIM_CHAMFER))
if R_CORNER > 0:
    outer = outer.edges("|Z").fillet(R_CORNER)
inner = (cq.Workplane("XY").workplane(offset=T_FLOOR)
         .rect(L - 2 * T_WALL, W - 2 * T_WALL).extrude(H))
body = outer.cut(inner)

# ---------------- posts ----------------
def post(x, y, d, top_z, flare_w, flare_h, fillet=False):
    """round post standing on the floor; its foot is either a concave fillet
    (fillet=True, radius flare_w) or a cone (radial growth flare_w over flare_h)"""
    r = d / 2.0
    h = top_z - T_FLOOR
    wp = (cq.Workplane("XZ")
          .moveTo(0, -0.01)
          .lineTo(r + flare_w, -0.01)
          .lineTo(r + flare_w, 0))
    if fillet:
        k = flare_w * (1 - 0.70710678)
        wp = wp.threePointArc((r + k, k), (r, flare_w))
    else:
        wp = wp.lineTo(r, flare_h)
    p = (wp.lineTo(r, h)
         .lineTo(0, h)
         .close()
         .revolve(360, (0, 0, 0), (0, 1, 0)))
    return p.translate((x, y, T_FLOOR))


posts = []
for sx in (-1, 1):
    for sy in (-1, 1):
        cx = sx * (L / 2 - POST_INSET)
        cy = sy * (W / 2 - POST_INSET)
        posts.append((cx, cy))
for (cx, cy) in posts:
    body = body.union(post(cx, cy, POST_D, POST_TOP, POST_FILLET, 0, fillet=True))
body = body.union(post(POST2_X, POST2_Y, POST_D, POST2_TOP, POST_FILLET, 0, fillet=True))
for (bx, by) in BOSS_PTS:
    body = body.union(post(bx, by, BOSS_D, T_FLOOR + BOSS_H, BOSS_FLARE_W, BOSS_FLARE_H))

# ---------------- divider ----------------
_k = 1 - 0.70710678
divider = (cq.Workplane("XZ", origin=(0, W / 2 - T_WALL + 0.01, 0))
           .moveTo(DIV_X - DIV_T / 2 - DIV_FILLET, T_FLOOR - 0.01)
           .lineTo(DIV_X + DIV_T / 2 + DIV_FILLET, T_FLOOR - 0.01)
           .lineTo(DIV_X + DIV_T / 2 + DIV_FILLET, T_FLOOR)
           .threePointArc((DIV_X + DIV_T / 2 + DIV_FILLET * _k, T_FLOOR + DIV_FILLET * _k),
                          (DIV_X + DIV_T / 2, T_FLOOR + DIV_FILLET))
           .lineTo(DIV_X + DIV_T / 2, H)
           .lineTo(DIV_X - DIV_T / 2, H)
           .lineTo(DIV_X - DIV_T / 2, T_FLOOR + DIV_FILLET)
           .threePointArc((DIV_X - DIV_T / 2 - DIV_FILLET * _k, T_FLOOR + DIV_FILLET * _k),
                          (DIV_X - DIV_T / 2 - DIV_FILLET, T_FLOOR))
           .close()
           .extrude(W - 2 * T_WALL + 0.02))
body = body.union(divider)

# ---------------- tabs ----------------
for sx in (-1, 1):
    xw = sx * L / 2
    pts = [(xw, -TAB_BASE / 2), (xw + sx * TAB_OUT, -TAB_TIP / 2),
           (xw + sx * TAB_OUT, TAB_TIP / 2), (xw, TAB_BASE / 2)]
    tab = (cq.Workplane("XY").polyline(pts).close().extrude(TAB_T)
           .edges("|Z").edges(cq.selectors.BoxSelector(
               (xw + sx * (TAB_OUT - 0.1), -TAB_TIP, -1), (xw + sx * (TAB_OUT + 0.1), TAB_TIP, TAB_T + 1)))
           .fillet(TAB_CORNER_R))
    # round the upper outer edges of the tab (not the one against the wall)
    tab = (tab.edges(cq.selectors.BoxSelector(
               (xw + sx * 0.5, -TAB_BASE, TAB_T - 0.1), (xw + sx * (TAB_OUT + 1), TAB_BASE, TAB_T + 0.1)))
           .fillet(TAB_EDGE_R))
    body = body.union(tab)
    # concave fillet between the tab and the end wall, trimmed to the tab outline
    strip = (cq.Workplane("XZ")
             .moveTo(xw, TAB_T)
             .lineTo(xw + sx * TAB_FILLET, TAB_T)
             .threePointArc((xw + sx * TAB_FILLET * (1 - 0.70710678), TAB_T + TAB_FILLET * (1 - 0.70710678)),
                            (xw, TAB_T + TAB_FILLET))
             .close()
             .extrude(TAB_BASE / 2, both=True))
    foot = (cq.Workplane("XY").polyline(pts).close().offset2D(-TAB_EDGE_R)
            .extrude(TAB_T + TAB_FILLET + 1))
    body = body.union(strip.intersect(foot))

# ---------------- holes ----------------
def cone(x, y, z0, r0, z1, r1):
    """true conical solid between (z0, r0) and (z1, r1) on a vertical axis"""
    return cq.Workplane("XY").add(
        cq.Solid.makeCone(r0, r1, z1 - z0, cq.Vector(x, y, z0), cq.Vector(0, 0, 1)))


def csk_from_top(x, y, z_top, hole_d, csk_d):
    """90 deg countersink opening upwards at z_top (overshoots both ends)"""
    ch = (csk_d - hole_d) / 2
    return cone(x, y, z_top - ch - 0.3, hole_d / 2 - 0.3, z_top + 0.5, csk_d / 2 + 0.5)


# corner & right-compartment post holes (blind, countersunk)
for (cx, cy, tz) in [(px, py, POST_TOP) for (px, py) in posts] + [(POST2_X, POST2_Y, POST2_TOP)]:
    hole = (cq.Workplane("XY").workplane(offset=tz - POST_HOLE_DEPTH)
            .center(cx, cy).circle(POST_HOLE_D / 2).extrude(POST_HOLE_DEPTH + 1))
    body = body.cut(hole).cut(csk_from_top(cx, cy, tz, POST_HOLE_D, POST_CSK_D))
# stand-off through holes, countersunk from the underside
for (bx, by) in BOSS_PTS:
    hole = (cq.Workplane("XY").workplane(offset=-1)
            .center(bx, by).circle(BOSS_HOLE_D / 2).extrude(T_FLOOR + BOSS_H + 2))
    ch = (BOSS_CSK_D - BOSS_HOLE_D) / 2
    body = body.cut(hole).cut(cone(bx, by, -0.5, BOSS_CSK_D / 2 + 0.5, ch + 0.3, BOSS_HOLE_D / 2 - 0.3))
# tab holes, countersunk from the top
for sx in (-1, 1):
    for sy in (-1, 1):
        hx = sx * (L / 2 + TAB_HOLE_X)
        hy = sy * TAB_HOLE_Y
        hole = (cq.Workplane("XY").workplane(offset=-1).center(hx, hy)
                .circle(TAB_HOLE_D / 2).extrude(TAB_T + 2))
        body = body.cut(hole).cut(csk_from_top(hx, hy, TAB_T, TAB_HOLE_D, TAB_CSK_D))

# ---------------- connector cut-outs in the front wall ----------------
# each port: a shallow recess (rectangle + latch notch) in the outer face and a
# slightly shorter through opening behind it
def port_profile(origin_y, depth, cx, w):
    """rectangle with a latch notch on top (rounded shoulders), drawn on an XZ
    plane at origin_y and extruded towards -Y by depth"""
    zt = CUT_Z0 + CUT_H
    nw = NOTCH_W / 2
    r = NOTCH_R
    c = r * (1 - 0.70710678)
    return (cq.Workplane("XZ", origin=(0, origin_y, 0))
            .moveTo(cx - w / 2, CUT_Z0)
            .lineTo(cx + w / 2, CUT_Z0)
            .lineTo(cx + w / 2, zt)
            .lineTo(cx + nw + r, zt)
            .threePointArc((cx + nw + c, zt + c), (cx + nw, zt + r))
            .lineTo(cx + nw, zt + NOTCH_H)
            .lineTo(cx - nw, zt + NOTCH_H)
            .lineTo(cx - nw, zt + r)
            .threePointArc((cx - nw - c, zt + c), (cx - nw - r, zt))
            .lineTo(cx - w / 2, zt)
            .close()
            .extrude(depth))


for (cx, w) in CUTS:
    # outer recess (open to the outside)
    recess_out = port_profile(-W / 2 + CUT_RECESS, CUT_RECESS + 1.0, cx, w)
    # inner recess (open to the inside)
    recess_in = port_profile(-W / 2 + T_WALL + 1.0, CUT_RECESS_IN + 1.0, cx, w)
    through = (cq.Workplane("XY")
               .box(w, T_WALL + 2.0, CUT_H - CUT_LIP)
               .translate((cx, -W / 2 + T_WALL / 2, CUT_Z0 + (CUT_H - CUT_LIP) / 2)))
    body = body.cut(recess_out).cut(recess_in).cut(through)

# window in the back wall
bw = (cq.Workplane("XY").box(BACK_WIN_W, T_WALL + 2, BACK_WIN_H)
      .translate((BACK_WIN_X, W / 2 - T_WALL / 2, BACK_WIN_Z0 + BACK_WIN_H / 2)))
body = body.cut(bw)
# window in the divider
dw = (cq.Workplane("XY").box(DIV_T + 2, DIV_WIN_S, DIV_WIN_S)
      .translate((DIV_X, DIV_WIN_Y, DIV_WIN_Z)))
body = body.cut(dw)

result = body
